import cadquery as cq

# ---------------------------------------------------------------
# Programmable brick (EV3-style) - driving dimensions (mm)
# X = width, Y = length (ports "1-4" at -Y, screen towards +Y), Z = up
# ---------------------------------------------------------------
W = 73.7            # main body width (X)
L = 120.0           # main body length (Y)
HW = W / 2.0
HL = L / 2.0

Z_BAT = 7.6         # top of battery pack / bottom of lower body
Z_LOW = 21.3        # top of lower body / bottom of upper body
Z_TOP = 38.0        # main top surface

# battery pack
BAT_W = 56.2
BAT_Y0, BAT_Y1 = -55.7, 52.9
BAT_CH_Y, BAT_CH_Z = 4.3, 3.1

# lower body
LOW_FRONT = -60.6   # lower body protrudes slightly at the front
COL_W = 3.15        # corner column width
BAND_HW = HW - COL_W
BAND_DEPTH = 1.6    # recess of the front / back band
BAND_CH = 0.9
LOW_CH_Y, LOW_CH_Z = 3.0, 4.6   # chamfer at the bottom of the corner columns
REB_Z, REB_D, REB_Y = 9.9, 0.6, 45.8   # rebate along the lower side edges
SLOT_Z0, SLOT_Z1, SLOT_Y1 = 9.35, 10.15, 54.0

# side panels
SP_T = 3.35
SP_Y0, SP_Y1 = -36.0, 34.9
SP_Z0 = 17.7
TAB_Z0 = 11.8
TABS = [(-30.6, -13.6), (11.2, 28.6)]

# screen plate
SCR_Y0 = 3.0
SCR_TOP = 41.6
SCR_OUT = (-0.85, 30.6, 55.7, 43.2)     # cx, cy, w, h
SCR_IN = (-1.65, 31.5, 44.5, 35.7)
SCR_D1, SCR_D2 = 1.2, 0.35
SCR_SLOPE = 0.85   # run of the sloped front wall of the display recess

# buttons
DP_C = (0.6, -21.0)
DP_TOP = 42.0
DP_HH = 17.25       # hexagon half height (Y)
DP_HW_END = 6.65    # hexagon half width at its flat ends
DP_HW_MID = 13.8    # hexagon half width at middle
DP_LOBE_R = 7.8
DP_LOBE_DX = 12.0
DP_LOBE_DY = -1.0   # lobes sit slightly towards the front
DP_FIL = 1.0
CB_W, CB_H, CB_TOP = 10.5, 9.8, 45.1
BB_X0, BB_X1, BB_Y0, BB_Y1, BB_TOP, BB_CH = -34.4, -22.1, -10.3, -0.2, 43.5, 2.6

# ports
PORT_W = 8.9
PORT_Z0 = 24.3
PORT_DEPTH = 5.5
FRONT_PORTS = [-23.55, -7.85, 7.85, 23.55]
BACK_PORTS = [11.6, 1.05, -9.5, -20.05]

SEAM = 0.35
NAME_D = 2.5      # emboss height of the name plate lettering


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def port_cutter(cx, y_face, direction):
    """RJ style port opening (L shape with latch tab) cut into a Y face.
    direction = -1 for the front face (-Y), +1 for the back face (+Y)."""
    s = 1 if direction < 0 else -1      # mirror so the step is on viewer's right
    pts = [(0, 0), (8.9, 0), (8.9, 8.4), (7.85, 8.4), (7.85, 9.3),
           (5.76, 9.3), (5.76, 8.4), (3.9, 8.4), (3.9, 5.0), (0, 5.0)]
    pts = [(cx + s * (x - PORT_W / 2.0), PORT_Z0 + z) for (x, z) in pts]
    solid = cq.Workplane("XZ").polyline(pts).close().extrude(PORT_DEPTH + 1.0)
    if direction < 0:
        solid = solid.mirror("XZ").translate((0, y_face - 1.0, 0))
    else:
        solid = solid.translate((0, y_face + 1.0, 0))
    return solid


def text_solid(txt, w, h, depth, kind="bold"):
    """Text extruded along +Z, scaled to a w x h box centred on the origin."""
    t = cq.Workplane("XY").text(txt, 10.0, depth, combine=False, kind=kind,
                                font="DejaVu Sans", halign="center", valign="center")
    s = t.val()
    bb = s.BoundingBox()
    sx, sy = w / bb.xlen, h / bb.ylen
    m = cq.Matrix([[sx, 0, 0, -bb.center.x * sx],
                   [0, sy, 0, -bb.center.y * sy],
                   [0, 0, 1, 0]])
    return cq.Workplane("XY").add(s.transformGeometry(m))


def on_face(solid, face):
    """Orient a text solid (built in XY, extruded +Z) onto a face.
    face: 'front' (-Y), 'back' (+Y), 'left' (-X), 'right' (+X), 'top'."""
    if face == "top":
        return solid
    s = solid.rotate((0, 0, 0), (1, 0, 0), 90)          # (x,y,z)->(x,-z,y)
    if face == "front":
        return s
    if face == "back":
        return s.rotate((0, 0, 0), (0, 0, 1), 180)
    if face == "left":
        return s.rotate((0, 0, 0), (0, 0, 1), -90)
    return s.rotate((0, 0, 0), (0, 0, 1), 90)


class NearXY(cq.Selector):
    """Select objects whose centre lies close (in XY) to one of the given points."""

    def __init__(self, pts, tol):
        self.pts = pts
        self.tol = tol

    def filter(self, objectList):
        out = []
        for o in objectList:
            c = o.Center()
            if any((c.x - px) ** 2 + (c.y - py) ** 2 < self.tol ** 2 for (px, py) in self.pts):
                out.append(o)
        return out


def junction(hw_end, hh, hw_mid, cxl, cyl, r):
    """Intersection of the upper hexagon flank (hw_end,hh)->(hw_mid,0)
    with the side lobe circle centred at (cxl, cyl)."""
    lo, hi = 0.0, 1.0

    def f(t):
        return ((hw_end + (hw_mid - hw_end) * t - cxl) ** 2
                + (hh - hh * t - cyl) ** 2 - r * r)
    for _ in range(60):
        m = 0.5 * (lo + hi)
        if f(m) > 0:
            lo = m
        else:
            hi = m
    t = 0.5 * (lo + hi)
    return (hw_end + (hw_mid - hw_end) * t, hh - hh * t)


# ---------------------------------------------------------------
# battery pack (underside)
# ---------------------------------------------------------------
battery = box(-BAT_W / 2, BAT_W / 2, BAT_Y0, BAT_Y1, 0, Z_BAT + 0.5)
battery = battery.edges("|X and <Z").chamfer(BAT_CH_Z, BAT_CH_Y)

# ---------------------------------------------------------------
# lower body
# ---------------------------------------------------------------
lower = box(-HW, HW, LOW_FRONT, HL, Z_BAT, Z_LOW + 0.2)
lower = lower.edges("|X and <Z").chamfer(LOW_CH_Z, LOW_CH_Y)
# recessed bands front and back (between the corner columns)
lower = lower.cut(box(-BAND_HW, BAND_HW, LOW_FRONT - 1, LOW_FRONT + BAND_DEPTH, Z_BAT - 1, Z_LOW + 1))
lower = lower.cut(box(-BAND_HW, BAND_HW, HL - BAND_DEPTH, HL + 1, Z_BAT - 1, Z_LOW - SEAM))
# refill so that the band itself keeps a square bottom edge (chamfer only on columns)
lower = lower.union(box(-BAND_HW, BAND_HW, LOW_FRONT + BAND_DEPTH, HL - BAND_DEPTH, Z_BAT, Z_LOW))
# small chamfer along the bottom edge of both bands
for yb_, sgn in ((LOW_FRONT + BAND_DEPTH, 1), (HL - BAND_DEPTH, -1)):
    wedge = (cq.Workplane("YZ", origin=(-BAND_HW, 0, 0))
             .polyline([(yb_ - sgn * 0.01, Z_BAT - 0.01), (yb_ + sgn * BAND_CH, Z_BAT - 0.01),
                        (yb_ - sgn * 0.01, Z_BAT + BAND_CH)]).close()
             .extrude(2 * BAND_HW))
    lower = lower.cut(wedge)
# rebate along the bottom of the long sides and short slots at both ends
for sx in (-1, 1):
    xa, xb = (HW - REB_D, HW + 1) if sx > 0 else (-HW - 1, -HW + REB_D)
    lower = lower.cut(box(xa, xb, -REB_Y, REB_Y, Z_BAT - 1, REB_Z))
    xa, xb = (HW - 0.8, HW + 1) if sx > 0 else (-HW - 1, -HW + 0.8)
    for sy in (-1, 1):
        ya, yb = (REB_Y, SLOT_Y1) if sy > 0 else (-SLOT_Y1, -REB_Y)
        lower = lower.cut(box(xa, xb, ya, yb, SLOT_Z0, SLOT_Z1))

# ---------------------------------------------------------------
# upper body
# ---------------------------------------------------------------
upper = box(-HW, HW, -HL, HL, Z_LOW, Z_TOP)

body = lower.union(upper).union(battery)

# side panels with downward tabs
for sx in (-1, 1):
    x0, x1 = (HW - 0.5, HW + SP_T) if sx > 0 else (-HW - SP_T, -HW + 0.5)
    panel = box(x0, x1, SP_Y0, SP_Y1, SP_Z0, Z_TOP)
    for (ty0, ty1) in TABS:
        panel = panel.union(box(x0, x1, ty0, ty1, TAB_Z0, SP_Z0 + 0.1))
    body = body.union(panel)

# seam grooves (front block split and upper/lower split)
body = body.cut(box(-HW - 5, HW + 5, -45.7 - SEAM / 2, -45.7 + SEAM / 2, Z_TOP - SEAM, Z_TOP + 1))
for sx in (-1, 1):
    xa, xb = (HW - SEAM, HW + 1) if sx > 0 else (-HW - 1, -HW + SEAM)
    body = body.cut(box(xa, xb, -45.7 - SEAM / 2, -45.7 + SEAM / 2, Z_LOW, Z_TOP + 1))
    body = body.cut(box(xa, xb, -HL - 1, SP_Y0, Z_LOW - SEAM / 2, Z_LOW + SEAM / 2))
    body = body.cut(box(xa, xb, SP_Y1, HL + 1, Z_LOW - SEAM / 2, Z_LOW + SEAM / 2))

# ---------------------------------------------------------------
# screen plate with recessed display
# ---------------------------------------------------------------
screen = box(-HW, HW, SCR_Y0, HL, Z_TOP - 0.1, SCR_TOP)
cx, cy, sw, sh = SCR_OUT
# outer display recess: its front (-Y) wall is sloped
y0, y1 = cy - sh / 2, cy + sh / 2
recess = (cq.Workplane("YZ", origin=(cx - sw / 2, 0, 0))
          .polyline([(y0, SCR_TOP + 1), (y0, SCR_TOP), (y0 + SCR_SLOPE, SCR_TOP - SCR_D1),
                     (y1, SCR_TOP - SCR_D1), (y1, SCR_TOP + 1)]).close()
          .extrude(sw))
screen = screen.cut(recess)
cx, cy, sw, sh = SCR_IN
screen = screen.cut(box(cx - sw / 2, cx + sw / 2, cy - sh / 2, cy + sh / 2,
                        SCR_TOP - SCR_D1 - SCR_D2, SCR_TOP + 1))
body = body.union(screen)
# seam line where the screen plate meets the housing (sides and back)
for sx in (-1, 1):
    xa, xb = (HW - SEAM, HW + 1) if sx > 0 else (-HW - 1, -HW + SEAM)
    body = body.cut(box(xa, xb, SP_Y1, HL + 1, Z_TOP - SEAM / 2, Z_TOP + SEAM / 2))
body = body.cut(box(-HW - 1, HW + 1, HL - SEAM, HL + 1, Z_TOP - SEAM / 2, Z_TOP + SEAM / 2))

# ---------------------------------------------------------------
# buttons
# ---------------------------------------------------------------
dx, dy = DP_C
ux, uy = junction(DP_HW_END, DP_HH, DP_HW_MID, DP_LOBE_DX, DP_LOBE_DY, DP_LOBE_R)
lx, ly = junction(DP_HW_END, DP_HH, DP_HW_MID, DP_LOBE_DX, -DP_LOBE_DY, DP_LOBE_R)
ly = -ly
dpad = (cq.Workplane("XY").workplane(offset=Z_TOP - 0.1).center(dx, dy)
        .moveTo(-DP_HW_END, DP_HH).lineTo(DP_HW_END, DP_HH).lineTo(ux, uy)
        .threePointArc((DP_LOBE_DX + DP_LOBE_R, DP_LOBE_DY), (lx, ly))
        .lineTo(DP_HW_END, -DP_HH).lineTo(-DP_HW_END, -DP_HH).lineTo(-lx, ly)
        .threePointArc((-DP_LOBE_DX - DP_LOBE_R, DP_LOBE_DY), (-ux, uy)).close()
        .extrude(DP_TOP - Z_TOP + 0.1))
# round only the concave junctions between the hexagon and the lobes
jpts = [(dx + ux, dy + uy), (dx + lx, dy + ly), (dx - ux, dy + uy), (dx - lx, dy + ly)]
dpad = dpad.edges(NearXY(jpts, 0.3)).fillet(DP_FIL)
body = body.union(dpad)

centre_btn = box(dx + 0.2 - CB_W / 2, dx + 0.2 + CB_W / 2, dy - 0.2 - CB_H / 2, dy - 0.2 + CB_H / 2,
                 Z_TOP, CB_TOP)
body = body.union(centre_btn)

back_btn = box(BB_X0, BB_X1, BB_Y0, BB_Y1, Z_TOP - 0.1, BB_TOP)
back_btn = back_btn.edges("|Z and >X and <Y").chamfer(BB_CH)
body = body.union(back_btn)

# ---------------------------------------------------------------
# ports
# ---------------------------------------------------------------
for px in FRONT_PORTS:
    body = body.cut(port_cutter(px, -HL, -1))
for px in BACK_PORTS:
    body = body.cut(port_cutter(px, HL, 1))

# mini-USB (PC) port on the back face
pc = (cq.Workplane("XZ")
      .polyline([(24.1, 27.2), (29.3, 27.2), (30.5, 29.6), (30.5, 30.8),
                 (22.9, 30.8), (22.9, 29.6)]).close()
      .extrude(-6.0).translate((0, HL - 5.0, 0)))
body = body.cut(pc)

# USB + SD slots on the -X side panel
XL = -HW - SP_T
body = body.cut(box(XL - 1, XL + 4.0, 3.6, 16.6, 24.0, 27.0))
body = body.cut(box(XL - 1, XL + 3.0, -20.2, -6.2, 24.8, 25.9))

# speaker grille on the +X side panel
GR_Y, GR_Z = 0.3, 26.4
rows = [(5.2, [(-3.1, 3.1)]), (3.5, [(-5.5, 5.5)]),
        (1.75, [(-8.8, -2.7), (2.7, 8.8)]), (0.0, [(-8.4, -2.3), (2.3, 8.4)]),
        (-1.75, [(-8.0, -1.8), (1.8, 8.0)]), (-3.5, [(-5.4, 5.4)]), (-5.2, [(-3.1, 3.1)])]
for (dz, segs) in rows:
    for (a, b) in segs:
        body = body.cut(box(HW + SP_T - 0.8, HW + SP_T + 1, GR_Y + a, GR_Y + b,
                            GR_Z + dz - 0.35, GR_Z + dz + 0.35))

# ---------------------------------------------------------------
# lettering and logos (plain extruded text)
# ---------------------------------------------------------------
try:
    yb = LOW_FRONT + BAND_DEPTH
    # name plate on the lower front band (raised)
    t = on_face(text_solid("BRIAN NGUYEN", 38.7, 4.5, NAME_D + 0.1), "front").translate((0.95, yb + 0.1, 15.05))
    body = body.union(t)
    # engraved port numbers under the front ports
    for i, px in enumerate(FRONT_PORTS):
        t = on_face(text_solid(str(i + 1), 1.2, 1.8, 1.0), "front").translate((px, -HL + 0.4, 23.0))
        body = body.cut(t)
    # engraved port letters under the back ports and "PC" label
    for i, px in enumerate(BACK_PORTS):
        t = on_face(text_solid("DCBA"[i], 1.7, 1.7, 1.0), "back").translate((px, HL - 0.4, 23.0))
        body = body.cut(t)
    t = on_face(text_solid("PC", 3.6, 1.8, 1.0), "back").translate((26.7, HL - 0.4, 25.0))
    body = body.cut(t)
    # engraved labels on the -X side panel
    t = on_face(text_solid("USB", 6.5, 3.0, 1.0), "left").translate((XL + 0.4, 10.1, 21.75))
    body = body.cut(t)
    t = on_face(text_solid("SD", 4.4, 3.0, 1.0), "left").translate((XL + 0.4, -13.7, 21.75))
    body = body.cut(t)
    # engraved "EV3" on the top of the front block
    t = text_solid("EV3", 14.7, 10.6, 1.5).translate((-26.2, -52.1, Z_TOP - 0.7))
    body = body.cut(t)
    # engraved badge with raised lettering on the top of the front block
    badge = (cq.Workplane("XY").workplane(offset=Z_TOP - 0.6).center(27.3, -52.1)
             .rect(9.2, 9.9).extrude(1.0).edges("|Z").fillet(1.0))
    body = body.cut(badge)
    t = text_solid("LEGO", 7.4, 4.0, 0.5, kind="bold").translate((27.3, -52.1, Z_TOP - 0.65))
    body = body.union(t)
except Exception:
    pass

result = body
